import math
import cadquery as cq

# Straight-knurled ring (axis along Y):
#   * plain front flange (facing -Y)
#   * straight knurl band behind it: axial trapezoidal grooves cut into a cylinder
#   * through bore
#   * 4 small blind holes in the back face (+Y) at 0/90/180/270 deg

# ---------------- driving dimensions (mm) ----------------
OD_FLANGE   = 100.0      # outer diameter of the plain front flange
ID_BORE     = 79.4       # bore diameter
T_TOTAL     = 8.0        # overall axial thickness
T_FLANGE    = 1.8        # axial thickness of the front flange

OD_KNURL    = 97.0       # knurl crest (tip) diameter
N_TEETH     = 158        # number of straight knurl teeth
KNURL_DEPTH = 0.8        # groove depth
GROOVE_TOP  = 0.60       # groove width at the crest circle  (fraction of pitch)
GROOVE_ROOT = 0.25       # groove width at the root circle   (fraction of pitch)
PHASE_DEG   = 1.13       # angle of the first tooth centre (from +X towards +Z)

HOLE_D      = 3.0        # blind hole diameter (back face)
HOLE_DEPTH  = 2.5        # blind hole depth
HOLE_R      = 43.8       # radius of the hole centre circle
N_HOLES     = 4

# ---------------- derived ----------------
R_TIP = OD_KNURL / 2
R_ROOT = R_TIP - KNURL_DEPTH
L_KNURL = T_TOTAL - T_FLANGE
PITCH = 2 * math.pi * R_TIP / N_TEETH

# ---------------- build with the ring axis along Z (front face at z=0) ----------------
flange = (cq.Workplane("XY")
          .circle(OD_FLANGE / 2).circle(ID_BORE / 2)
          .extrude(T_FLANGE))

band = (cq.Workplane("XY").workplane(offset=T_FLANGE)
        .circle(R_TIP).circle(ID_BORE / 2)
        .extrude(L_KNURL))

body = flange.union(band)

# one trapezoidal groove (cross-section in the XY plane), extended past the crest
ht = GROOVE_TOP * PITCH / 2
hr = GROOVE_ROOT * PITCH / 2
r_out = R_TIP + 0.4
h_out = hr + (ht - hr) * (r_out - R_ROOT) / (R_TIP - R_ROOT)
groove = (cq.Workplane("XY").workplane(offset=T_FLANGE)
          .polyline([(R_ROOT, -hr), (r_out, -h_out), (r_out, h_out), (R_ROOT, hr)])
          .close()
          .extrude(L_KNURL + 0.01)
          .val())

# polar pattern: grooves sit half a pitch from the tooth centres.
# (the final -90 deg turn about X maps model angle a to -a in the XZ plane)
cutters = [groove.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1),
                         -PHASE_DEG - (i + 0.5) * 360.0 / N_TEETH)
           for i in range(N_TEETH)]
body = body.cut(cq.Workplane("XY").add(cq.Compound.makeCompound(cutters)))

# blind holes in the back face, on the model X and Y axes (-> X and Z after orientation)
holes = (cq.Workplane("XY").workplane(offset=T_TOTAL - HOLE_DEPTH)
         .polarArray(HOLE_R, 0, 360, N_HOLES)
         .circle(HOLE_D / 2)
         .extrude(HOLE_DEPTH + 0.01))
body = body.cut(holes)

# ---------------- orient: ring axis along +Y, flange facing -Y (front) ----------------
# rotation about X by -90 deg maps (x, y, z) -> (x, z, -y)
result = body.rotate((0, 0, 0), (1, 0, 0), -90)

VIEW = {"azimuth": 45, "elevation": 26}
